import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 150.0          # overall width  (X)
D = 24.6           # overall depth  (Y), front face at Y=0, open at back
H = 120.5          # overall height (Z) of the front plate
T = 3.4            # wall thickness
R_OUT = 4.1        # outer round: vertical front corners + bottom edges
WALL_DROP = 3.6    # side walls are lower than the front plate by this much

# X-window pattern in the front plate (centre of the cross; the pattern is
# deliberately offset from the plate centre, as on the original part)
CX = -4.1
CZ = 51.1
WIN_L = 47.5       # window extent left of cross centre
WIN_R = 49.8       # window extent right of cross centre
WIN_T = 34.1       # window extent above cross centre
WIN_B = 33.8       # window extent below cross centre
BAR_SLOPE = 0.673  # dz/dx of the diagonal bars
BAR_W = 14.4       # perpendicular width of each diagonal bar

# standoff bosses on the inside of the front plate
BOSS_CX = -4.25    # boss pattern centre (X)
BOSS_DX = 60.9     # half spacing in X about BOSS_CX
BOSS_DZ = 41.75    # half spacing in Z about CZ
BOSS_D = 8.5
BOSS_LEN = 14.3    # protrusion from plate inner face
BOSS_HOLE_D = 3.3
BOSS_HOLE_DEPTH = 10.0
BOSS_FILLET = 3.6
BOSS_CHAMFER = 0.5

# holes in the floor
FLOOR_HOLE_D = 9.8
FLOOR_HOLE_X = 28.4
FLOOR_HOLE_Y = 11.4
SLOT_Y = 19.2      # double-D slot position (from front face)
SLOT_L = 13.7
SLOT_W = 6.9
SLOT_BAR = 2.5

# ---------------- body: U-channel with floor ----------------
outer = cq.Workplane("XY").box(W, D, H, centered=(True, False, False))
# round the outer edges in one go: both vertical front corners plus the
# front/side bottom edges (gives clean spherical corner blends)
round_edges = [
    e for e in outer.edges().vals()
    if (abs(e.Center().z) < 1e-6 and e.Center().y < D - 1e-6)
    or (abs(e.Center().y) < 1e-6 and abs(abs(e.Center().x) - W / 2.0) < 1e-6)
]
outer_s = outer.val().fillet(R_OUT, round_edges)
outer = cq.Workplane("XY").add(outer_s)
inner = (
    cq.Workplane("XY")
    .box(W - 2 * T, D + 2.0, H, centered=(True, False, False))
    .translate((0, T, T))
)
body = outer.cut(inner)

# side walls are a bit lower than the front plate
top_cut = (
    cq.Workplane("XY")
    .box(W + 10.0, D + 10.0, WALL_DROP + 5.0, centered=(True, False, False))
    .translate((0, T, H - WALL_DROP))
)
body = body.cut(top_cut)

# ---------------- X window in the front plate ----------------
win = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .center(CX + (WIN_R - WIN_L) / 2.0, CZ + (WIN_T - WIN_B) / 2.0)
    .rect(WIN_L + WIN_R, WIN_T + WIN_B)
    .extrude(-(T + 2.0))
    .translate((0, -1.0, 0))
)
bar_len = 2.0 * (WIN_L + WIN_R)
ang = math.degrees(math.atan(BAR_SLOPE))
bars = None
for a in (ang, -ang):
    b = (
        cq.Workplane("XZ")
        .center(CX, CZ)
        .rect(bar_len, BAR_W)
        .extrude(-(T + 4.0))
        .translate((0, -2.0, 0))
    )
    b = b.rotate((CX, 0, CZ), (CX, 1, CZ), -a)
    bars = b if bars is None else bars.union(b)
win = win.cut(bars)
body = body.cut(win)

# ---------------- standoff bosses ----------------
# revolved profile: root flare (concave round) + cylinder + end chamfer,
# slightly embedded into the plate so it fuses cleanly
def make_boss(bx, bz):
    r = BOSS_D / 2.0
    f = BOSS_FILLET
    c = BOSS_CHAMFER
    L = BOSS_LEN
    k = 1.0 - math.sqrt(0.5)
    prof = (
        cq.Workplane("XY")
        .moveTo(0.0, -1.0)
        .lineTo(r + f, -1.0)
        .lineTo(r + f, 0.0)
        .threePointArc((r + f * k, f * k), (r, f))
        .lineTo(r, L - c)
        .lineTo(r - c, L)
        .lineTo(0.0, L)
        .close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
    )
    boss = prof.translate((bx, T, bz))
    hole = (
        cq.Workplane("XZ", origin=(bx, T + L + 1.0, bz))
        .circle(BOSS_HOLE_D / 2.0)
        .extrude(BOSS_HOLE_DEPTH + 1.0)
    )
    return boss, hole


boss_holes = []
for sx in (-1, 1):
    for sz in (-1, 1):
        b, h = make_boss(BOSS_CX + sx * BOSS_DX, CZ + sz * BOSS_DZ)
        body = body.union(b)
        boss_holes.append(h)
for h in boss_holes:
    body = body.cut(h)

# ---------------- holes in the floor ----------------
floor_holes = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .pushPoints([(-FLOOR_HOLE_X, FLOOR_HOLE_Y), (FLOOR_HOLE_X, FLOOR_HOLE_Y)])
    .circle(FLOOR_HOLE_D / 2.0)
    .extrude(T + 2.0)
)
body = body.cut(floor_holes)

slot = (
    cq.Workplane("XY", origin=(0, SLOT_Y, -1.0))
    .slot2D(SLOT_L, SLOT_W, 0)
    .extrude(T + 2.0)
)
slot_bar = (
    cq.Workplane("XY", origin=(0, SLOT_Y, -2.0))
    .rect(SLOT_BAR, SLOT_W + 2.0)
    .extrude(T + 4.0)
)
body = body.cut(slot.cut(slot_bar))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
